import math
import cadquery as cq

# ================= driving dimensions (mm, degrees) =================
# Thin sheet-metal wall panel: an open (~150 deg) segment of a slightly
# elliptical cone that widens upwards.  The segment is trimmed by two
# parallel inclined rim planes (top and bottom), a small horizontal flat at
# the lowest part of the bottom rim, and two end planes.

T = 0.15                 # sheet thickness

# ---- cone (outer surface) ----
HALF_ANGLE = 11.85       # cone half angle (opens upwards)
AXIS_LEAN_Y = -2.146     # lean of the axis top towards +Y (neg. = towards -Y)
AXIS_LEAN_X = 0.257      # lean of the axis top towards +X
AXIS_Y = -58.91          # the axis passes through (0, AXIS_Y, 0)
R_REF = 89.07            # mean outer radius where the axis crosses z = 0
ELL_E = 0.0225           # ellipticity: semi-axes = R * (1 +/- ELL_E)
ELL_ANGLE = 124.27       # azimuth of the major axis (from +X towards +Y)

# ---- rim planes:  z = Z_AT_AXIS - tan(TILT) * (y - AXIS_Y) ----
RIM_TILT = 9.62          # both rim planes drop towards +Y (parallel planes)
TOP_Z = 74.90            # top rim plane height on the axis
BOT_Z = -60.71           # bottom rim plane height on the axis
BOT_FLAT_Z = -72.2       # horizontal flat trimming the lowest part of the bottom rim

# ---- azimuth of the end corners (about the cone axis, from +X towards +Y) ----
END_R_TOP = 16.62        # right (+X) end at the top rim
END_R_BOT = 13.89        # right (+X) end at the bottom rim
END_L_TOP = 164.76       # left (-X) end at the top rim
END_L_BOT = 160.97       # left (-X) end at the bottom rim

BIG = 600.0              # size of the trimming half-space blocks

# ================= derived geometry =================
ta = math.tan(math.radians(HALF_ANGLE))
AX = cq.Vector(math.tan(math.radians(AXIS_LEAN_X)),
               math.tan(math.radians(AXIS_LEAN_Y)), 1.0).normalized()   # cone axis
_x = cq.Vector(1.0, 0.0, 0.0)
EX = (_x - AX * _x.dot(AX)).normalized()          # azimuth 0 direction
EY = AX.cross(EX)                                  # azimuth 90 direction
P0 = cq.Vector(0.0, AXIS_Y, 0.0)
_m = math.radians(ELL_ANGLE)
U_MAJ = EX * math.cos(_m) + EY * math.sin(_m)     # major axis direction


def ell_factor(az_deg):
    """Polar radius of the (unit mean radius) ellipse at azimuth az_deg."""
    a, b = 1.0 + ELL_E, 1.0 - ELL_E
    psi = math.radians(az_deg - ELL_ANGLE)
    return a * b / math.sqrt((b * math.cos(psi)) ** 2 + (a * math.sin(psi)) ** 2)


def ell_wire(h, d_r):
    """Cross-section ellipse of the cone (perpendicular to the axis) at axial height h."""
    r = R_REF + h * ta - d_r
    # x-direction chosen so that the seam of the closed ellipse lies in the open gap
    e = cq.Edge.makeEllipse(r * (1 + ELL_E), r * (1 - ELL_E), P0 + AX * h, AX, -U_MAJ)
    return cq.Wire.assembleEdges([e])


def rim_plane(z_axis, tilt_deg):
    """(point, upward normal) of an inclined rim plane."""
    k = math.tan(math.radians(tilt_deg))
    return cq.Vector(0.0, AXIS_Y, z_axis), cq.Vector(0.0, k, 1.0).normalized()


def cone_point(az_deg, plane):
    """Point of the outer cone surface at azimuth az_deg lying on a plane."""
    p, n = plane
    az = math.radians(az_deg)
    radial = (EX * math.cos(az) + EY * math.sin(az)) * ell_factor(az_deg)
    base = P0 + radial * R_REF            # generator: base + dirv * h
    dirv = AX + radial * ta
    h = (p - base).dot(n) / dirv.dot(n)
    return base + dirv * h


def halfspace(p, n):
    """Large block occupying the side of the plane (p, n) that n points to."""
    n = n.normalized()
    xd = _x if abs(n.dot(_x)) < 0.9 else cq.Vector(0, 1, 0)
    xd = (xd - n * xd.dot(n)).normalized()
    pl = cq.Plane(origin=p, xDir=xd, normal=n)
    return cq.Workplane(pl).rect(BIG, BIG).extrude(BIG).val()


def azimuth_probe(az_deg):
    az = math.radians(az_deg)
    return P0 + (EX * math.cos(az) + EY * math.sin(az)) * R_REF


# ---- elliptic conical shell: ruled loft between two cross-section ellipses ----
H_LO, H_HI = -110.0, 110.0
outer = cq.Solid.makeLoft([ell_wire(H_LO, 0.0), ell_wire(H_HI, 0.0)], True)
d_t = T / math.cos(math.radians(HALF_ANGLE))
inner = cq.Solid.makeLoft([ell_wire(H_LO - 5.0, d_t), ell_wire(H_HI + 5.0, d_t)], True)
shell = outer.cut(inner)

# ---- rim trims ----
top_pl = rim_plane(TOP_Z, RIM_TILT)
bot_pl = rim_plane(BOT_Z, RIM_TILT)
shell = shell.cut(halfspace(top_pl[0], top_pl[1]))
shell = shell.cut(halfspace(bot_pl[0], -bot_pl[1]))
shell = shell.cut(halfspace(cq.Vector(0, 0, BOT_FLAT_Z), cq.Vector(0, 0, -1)))

# ---- end trims: planes through the end corners, parallel to the cone axis ----
rt = cone_point(END_R_TOP, top_pl)
rb = cone_point(END_R_BOT, bot_pl)
n_r = (rb - rt).cross(AX)
if n_r.dot(azimuth_probe(-60.0) - rt) < 0:
    n_r = -n_r
shell = shell.cut(halfspace(rt, n_r))

lt = cone_point(END_L_TOP, top_pl)
lb = cone_point(END_L_BOT, bot_pl)
n_l = (lb - lt).cross(AX)
if n_l.dot(azimuth_probe(240.0) - lt) < 0:
    n_l = -n_l
shell = shell.cut(halfspace(lt, n_l))

result = cq.Workplane("XY").newObject(shell.clean().Solids())

VIEW = {"azimuth": 45, "elevation": 26}
